"""U-shaped servo/pan bracket with a round hub boss.

Base plate (front, XZ plane) with a cylindrical boss pointing to -Y, two side
plates pointing to +Y with rounded ends.  The +X side plate carries a
four-arm servo-horn pocket on its inner face (arms break out through the top
and bottom edges), a centre bore and four horn-screw holes; the -X side plate
carries a single idler bore coaxial with it.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 64.0            # overall width of the U bracket (X)
H = 32.0            # height of the bracket (Z)
TB = 4.0            # base plate thickness (Y)
TS = 5.0            # side plate thickness (X)

BOSS_D = 24.5       # round boss on the front face
BOSS_L = 30.0       # boss length (towards -Y)
BOSS_BORE = 10.0    # central through bore of the boss
BOLT_PCR = 8.75     # bolt circle radius of the six boss holes
BOLT_D = 4.0        # boss hole diameter
BOLT_N = 6
BOLT_EDGE_R = 1.5   # rounded entry of the boss holes on the inner face of the base

HOLE_Y = 27.0       # side-plate bore centre, measured from the front face (Y=0)
ARC_R = 25.0        # radius of the rounded end of the side plates (centred on the bore)

RIGHT_BORE = 10.0       # servo side (+X) centre bore
RIGHT_SMALL_D = 2.0     # four horn screw holes
RIGHT_SMALL_OFF = 7.1   # half spacing of the horn screw square
RIGHT_SMALL_EDGE_R = 0.9  # rounded entry of the horn screw holes (outer face)
LEFT_BORE = 6.0         # idler side (-X) bore

HORN_DEPTH = 3.0    # depth of the horn pocket in the +X plate (from its inner face)
HORN_HUB_R = 11.5   # hub radius of the horn pocket
HORN_ARM_W = 7.8    # arm width (arms have rounded tips)
HORN_ARM_ANG = 45.0 # arm angle from the plate's long axis (deg)
HORN_ARM_R = 18.3   # distance from the centre to the arm tip-circle centre

BOSS_SEAM_ANG = 200.0  # where the boss cylinder's seam sits (cosmetic only)

# ---------------- base plate ----------------
body = cq.Workplane("XY").box(W, TB, H, centered=(True, False, True))

# ---------------- side plates (rounded ends centred on the bores) ----------------
y_arc = HOLE_Y + math.sqrt(ARC_R ** 2 - (H / 2) ** 2)


def side_plate(x0):
    return (
        cq.Workplane("YZ", origin=(x0, 0, 0))
        .moveTo(0, -H / 2)
        .lineTo(y_arc, -H / 2)
        .threePointArc((HOLE_Y + ARC_R, 0), (y_arc, H / 2))
        .lineTo(0, H / 2)
        .close()
        .extrude(TS)
    )


body = body.union(side_plate(-W / 2)).union(side_plate(W / 2 - TS))

# ---------------- hub boss on the front face ----------------
boss = (
    cq.Workplane("XZ")
    .transformed(rotate=(0, 0, BOSS_SEAM_ANG))
    .circle(BOSS_D / 2)
    .extrude(BOSS_L)
)
body = body.union(boss)

# boss bore + bolt circle, through boss and base plate
bolt_pts = [
    (BOLT_PCR * math.cos(math.radians(90 + i * 360 / BOLT_N)),
     BOLT_PCR * math.sin(math.radians(90 + i * 360 / BOLT_N)))
    for i in range(BOLT_N)
]


def axial_hole(plane, origin, dia, depth, seam_ang=90.0):
    """Plain cylindrical cutter; seam_ang only rotates the (cosmetic) seam line."""
    return (
        cq.Workplane(plane, origin=origin)
        .transformed(rotate=(0, 0, seam_ang))
        .circle(dia / 2)
        .extrude(depth)
    )


boss_holes = axial_hole("XZ", (0, TB + 1, 0), BOSS_BORE, BOSS_L + TB + 2)
for (px, pz) in bolt_pts:
    boss_holes = boss_holes.union(axial_hole("XZ", (px, TB + 1, pz), BOLT_D, BOSS_L + TB + 2))
body = body.cut(boss_holes)

# ---------------- side plate bores ----------------
left_bore = axial_hole("YZ", (-W / 2 - 1, HOLE_Y, 0), LEFT_BORE, TS + 2)
body = body.cut(left_bore)

small_pts = [(sy * RIGHT_SMALL_OFF, sz * RIGHT_SMALL_OFF) for sy in (-1, 1) for sz in (-1, 1)]
right_holes = axial_hole("YZ", (W / 2 - TS - 1, HOLE_Y, 0), RIGHT_BORE, TS + 2)
for (dy, dz) in small_pts:
    right_holes = right_holes.union(
        axial_hole("YZ", (W / 2 - TS - 1, HOLE_Y + dy, dz), RIGHT_SMALL_D, TS + 2))
body = body.cut(right_holes)

# ---------------- servo horn pocket on the inner face of the +X plate ----------------
x_in = W / 2 - TS
pocket = (
    cq.Workplane("YZ", origin=(x_in - 1, 0, 0))
    .center(HOLE_Y, 0)
    .circle(HORN_HUB_R)
    .extrude(HORN_DEPTH + 1)
)
for ang in (HORN_ARM_ANG, -HORN_ARM_ANG):
    arm = (
        cq.Workplane("YZ", origin=(x_in - 1, 0, 0))
        .center(HOLE_Y, 0)
        .slot2D(2 * HORN_ARM_R + HORN_ARM_W, HORN_ARM_W, ang)
        .extrude(HORN_DEPTH + 1)
    )
    pocket = pocket.union(arm)
body = body.cut(pocket)

# ---------------- rounded hole entries ----------------
def circle_edges(shape, radius, centres):
    """Circular edges of the given radius whose centres match one of `centres`."""
    found = []
    for e in shape.Edges():
        if e.geomType() != "CIRCLE" or abs(e.radius() - radius) > 1e-4:
            continue
        c = e.Center()
        for (cx, cy, cz) in centres:
            if abs(c.x - cx) < 1e-3 and abs(c.y - cy) < 1e-3 and abs(c.z - cz) < 1e-3:
                found.append(e)
                break
    return found


solid = body.val()

# horn screw holes: rounded on the outer face of the +X plate
small_centres = [(W / 2, HOLE_Y + dy, dz) for (dy, dz) in small_pts]
solid = solid.fillet(RIGHT_SMALL_EDGE_R, circle_edges(solid, RIGHT_SMALL_D / 2, small_centres))

# boss screw holes: rounded on the inner face of the base plate
bolt_centres = [(px, TB, pz) for (px, pz) in bolt_pts]
solid = solid.fillet(BOLT_EDGE_R, circle_edges(solid, BOLT_D / 2, bolt_centres))

result = cq.Workplane("XY").add(solid)
